import math
import cadquery as cq

# ---------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------
# Housing (box)
BW = 75.5          # width along X
BD = 117.7         # total depth along Y (front face at y=0)
BDF = 76.1         # depth of the full-width front portion
BH = 130.8         # height along Z (bottom at z=0)
BACK_X1 = 24.5     # left face of the rear portion (front part)
BACK_X2 = 30.0     # left face of the rear portion (rear part)
BACK_STEP_Y = 105.0
R_VERT = 0.0       # front-left vertical edge (sharp)
# -X side recess (pocket between a front flange, a top overhang and a bottom ledge)
REC_X = 24.5       # depth of recess face
REC_Y0, REC_Y1 = 5.5, 80.0   # front flange thickness / open to the rear
REC_Z0, REC_Z1 = 12.0, 126.0
REC_TOP_R = 6.0    # cove under the top overhang
REC_CORNER_R = 5.5 # vertical cove behind the front flange
TAB_X0, TAB_Y0, TAB_Y1 = 2.0, 5.5, 53.8
TAB_Z0, TAB_Z1 = 99.0, 104.7
SIDE_HOLES = [(75.4, 94.2), (48.1, 82.8), (60.8, 61.8), (41.8, 59.8)]
R_TOP = 7.0        # top / bottom edge round
R_VERT_R = 6.0     # vertical rounds on the +X side

# Top cover plate
TP_X0, TP_X1 = 1.5, 61.0
TP_Y0, TP_Y1 = 8.4, 74.4
TP_T = 1.6
TP_HOLES = [(15.3, 25.9, 8.0), (15.3, 45.2, 9.7), (15.3, 64.7, 12.5)]
TAB_HOLES = TP_HOLES[:2]

# Bottom plate
BP_X0, BP_X1 = 3.0, 63.7
BP_Y0, BP_Y1 = 11.3, 73.6
BP_T = 1.4

# Dovetail / V geometry
V_ANG = math.radians(40.0)   # flank angle from X axis
V_APEX = (16.0, 133.5)       # outer apex of the V tongue
V_T = 3.5                    # wall thickness of the V tongue
V_BASE_Y = 122.8             # y where the left arm of the tongue ends

# Rail (bar)
BAR_X0, BAR_X1 = -133.2, 60.5
BAR_Z0, BAR_Z1 = 31.0, 100.0
BAR_FRONT = 124.3            # main front face
BAR_LIP = BD                 # front face of the end lips (flush with housing back)
BAR_BACK = 142.8
RIB_BACK = 146.3             # protruding middle band on the back face
RIB_Z0, RIB_Z1 = 53.5, 77.5
LNOTCH_X = -114.7            # end of left lip
LNOTCH_DEPTH = 128.3         # apex y of the left notch

# Rod
ROD_X, ROD_Z, ROD_D = -120.5, 45.4, 9.2
ROD_END_Y = 237.8

# Knob on the rail end
KNOB_Y, KNOB_Z = 141.0, 65.6
KNOB_D, KNOB_L = 12.0, 13.5
KNOB_FL_D = 16.0

# Side (+X) face features
PANEL_Y0, PANEL_Y1 = 30.9, 97.0
PANEL_Z0, PANEL_Z1 = 35.5, 117.6
PANEL_T = 1.0
SCREW_Y, SCREW_Z = 53.3, 107.8
BOSS_Y, BOSS_Z, BOSS_D, BOSS_H = 60.7, 18.6, 19.5, 5.0
BOSS_TOP_D = 13.4
STRIP_Y0, STRIP_Y1 = 99.0, 112.5
STRIP_Z0, STRIP_Z1 = 9.9, 124.9
STRIP_T = 1.7

# Bottom boss
BB_X, BB_Y = TP_HOLES[0][0], TP_HOLES[0][1]
# Lever
LEV_X0, LEV_X1 = 34.3, 56.2
LEV_Y0, LEV_Y1 = 45.2, 61.7
LEV_BOT = -37.3
GRIP_D, NECK_D = 14.7, 8.7
GRIP_END_Y = 108.7
GRIP_DROP = 0.6


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def sel_box(x0, y0, z0, x1, y1, z1):
    return cq.selectors.BoxSelector((x0, y0, z0), (x1, y1, z1))


# ---------------------------------------------------------------
# Housing
# ---------------------------------------------------------------
def rounded_poly(plane, pts):
    """Closed polygon with per-corner tangent arcs. pts = [(u, v, r), ...]."""
    n = len(pts)
    segs = []
    for i in range(n):
        px, py, r = pts[i]
        ax, ay, _ = pts[i - 1]
        bx, by, _ = pts[(i + 1) % n]
        if r <= 0:
            segs.append(((px, py), None, (px, py)))
            continue
        ux, uy = ax - px, ay - py
        lu = math.hypot(ux, uy); ux, uy = ux / lu, uy / lu
        vx, vy = bx - px, by - py
        lv = math.hypot(vx, vy); vx, vy = vx / lv, vy / lv
        cosang = ux * vx + uy * vy
        ang = math.acos(max(-1.0, min(1.0, cosang)))
        d = r / math.tan(ang / 2)
        t1 = (px + ux * d, py + uy * d)
        t2 = (px + vx * d, py + vy * d)
        bxv, byv = ux + vx, uy + vy
        lb = math.hypot(bxv, byv); bxv, byv = bxv / lb, byv / lb
        dc = r / math.sin(ang / 2)
        cx, cy = px + bxv * dc, py + byv * dc
        mid = (cx - bxv * r, cy - byv * r)
        segs.append((t1, mid, t2))
    wp = cq.Workplane(plane).moveTo(*segs[0][2])
    for i in range(1, n + 1):
        t1, mid, t2 = segs[i % n]
        wp = wp.lineTo(*t1)
        if mid is not None:
            wp = wp.threePointArc(mid, t2)
    return wp.close()


# plan-view outline with vertical edge rounds
plan = [
    (0, 0, R_VERT), (BW, 0, R_VERT_R), (BW, BD, R_VERT_R), (BACK_X2, BD, 0),
    (BACK_X2, BACK_STEP_Y, 2.5), (BACK_X1, BACK_STEP_Y, 2.5), (BACK_X1, BDF, 3.0), (0, BDF, 0),
]
body = rounded_poly("XY", plan).extrude(BH)
# top and bottom edge rounds (the round runs around the tangent chain of the outline)
body = body.edges(sel_box(-1, -1, BH - 0.5, BW + 1, 0.5, BH + 0.5)).fillet(R_TOP)
body = body.edges(sel_box(-1, -1, -0.5, BW + 1, 0.5, 0.5)).fillet(R_TOP)

# recess on the -X side
body = body.cut(box(-1, REC_X, REC_Y0, REC_Y1, REC_Z0, REC_Z1))
body = body.edges("|Z").edges(sel_box(REC_X - 0.5, REC_Y0 - 0.5, REC_Z0 + 1, REC_X + 0.5, REC_Y0 + 0.5, REC_Z1 - 1)).fillet(REC_CORNER_R)
# concave round between the recess face and the underside of the top overhang
rr = REC_TOP_R
cove = (cq.Workplane("XZ").moveTo(REC_X - rr, REC_Z1).lineTo(REC_X + 0.2, REC_Z1)
        .lineTo(REC_X + 0.2, REC_Z1 - rr).lineTo(REC_X, REC_Z1 - rr)
        .threePointArc((REC_X - rr + rr * math.cos(math.radians(45)), REC_Z1 - rr + rr * math.sin(math.radians(45))),
                       (REC_X - rr, REC_Z1))
        .close())
# arc centre is (REC_X - rr, REC_Z1 - rr): the cove fills the corner outside that circle
cove = cove.extrude(-(BDF - REC_Y0 - 5.0)).translate((0, REC_Y0 + 5.0, 0))
body = body.union(cove)
# bracket tab inside the recess
tab = box(TAB_X0, REC_X + 0.5, TAB_Y0 - 0.5, TAB_Y1, TAB_Z0, TAB_Z1)
for hx, hy, hd in TAB_HOLES:
    tab = tab.cut(cq.Workplane("XY").circle(hd / 2).extrude(20).translate((hx, hy, TAB_Z0 - 5)))
body = body.union(tab)
# rounded front end of the slot between the tab and the top overhang
slot_r = (REC_Z1 - TAB_Z1) / 2
fill = box(0, REC_X + 0.5, REC_Y0 - 0.5, REC_Y0 + slot_r, TAB_Z1 - 0.1, REC_Z1 + 0.1)
fill = fill.cut(cq.Workplane("YZ").circle(slot_r).extrude(REC_X + 4)
                .translate((-2, REC_Y0 + slot_r, TAB_Z1 + slot_r)))
body = body.union(fill)
for hy, hz in SIDE_HOLES:
    body = body.cut(cq.Workplane("YZ").circle(3.2).extrude(6).translate((REC_X - 5, hy, hz)))

# V tongue (thin V-shaped wall at the rear-left corner)
t = 1.0 / math.tan(V_ANG)
ax, ay = V_APEX
iay = ay - V_T / math.cos(V_ANG)
yend = BD - R_TOP + 0.5
vwall_pts = [
    (ax - (ay - V_BASE_Y) * t, V_BASE_Y),
    (ax, ay),
    (ax + (ay - yend) * t, yend),
    (ax + (iay - BD) * t, BD),
    (ax, iay),
    (ax - (iay - V_BASE_Y) * t, V_BASE_Y),
]
vwall = cq.Workplane("XY").polyline(vwall_pts).close().extrude(BH)
body = body.union(vwall)

# top plate with three holes
top_plate = box(TP_X0, TP_X1, TP_Y0, TP_Y1, BH, BH + TP_T)
for hx, hy, hd in TP_HOLES:
    top_plate = top_plate.cut(
        cq.Workplane("XY").circle(hd / 2).extrude(TP_T + 10).translate((hx, hy, BH - 5)))
body = body.union(top_plate)
for hx, hy, hd in TP_HOLES:
    body = body.cut(cq.Workplane("XY").circle(hd / 2).extrude(20).translate((hx, hy, BH - 15)))

# bottom plate
bot_plate = box(BP_X0, BP_X1, BP_Y0, BP_Y1, -BP_T, 0.5)
body = body.union(bot_plate)
for hx, hy, hd in TP_HOLES[1:]:
    body = body.cut(cq.Workplane("XY").circle(hd / 2).extrude(REC_Z0 + 10).translate((hx, hy, -BP_T - 5)))

# ---------------------------------------------------------------
# +X side features
# ---------------------------------------------------------------
panel = box(BW - 0.5, BW + PANEL_T, PANEL_Y0, PANEL_Y1, PANEL_Z0, PANEL_Z1)
body = body.union(panel)
# counterbored screw in the panel
sx = BW + PANEL_T
body = body.cut(cq.Workplane("YZ").circle(7.0).extrude(0.6).translate((sx - 0.6, SCREW_Y, SCREW_Z)))
body = body.cut(cq.Workplane("YZ").circle(4.1).extrude(3).translate((sx - 3, SCREW_Y, SCREW_Z)))
body = body.union(box(sx - 3.2, sx - 2.0, SCREW_Y - 3.6, SCREW_Y + 3.6, SCREW_Z - 0.45, SCREW_Z + 0.45))

# lower round boss with hole
boss = (cq.Workplane("YZ").circle(BOSS_D / 2).workplane(offset=BOSS_H + 1)
        .circle(BOSS_TOP_D / 2).loft().translate((BW - 1, BOSS_Y, BOSS_Z)))
body = body.union(boss)
body = body.cut(cq.Workplane("YZ").circle(2.5).extrude(6).translate((BW + BOSS_H - 4, BOSS_Y, BOSS_Z)))

# vertical strip near the rear of the +X face
strip = box(BW - 0.5, BW + STRIP_T, STRIP_Y0, STRIP_Y1, STRIP_Z0, STRIP_Z1)
body = body.union(strip)
latch = box(BW + STRIP_T - 0.2, BW + STRIP_T + 3.2, 102.0, 108.8, 105.5, 114.9)
body = body.union(latch)
# connector block
conn = box(BW + STRIP_T - 0.2, BW + STRIP_T + 0.8, 99.5, 112.0, 11.3, 43.6)
body = body.union(conn)
cx = BW + STRIP_T + 0.8
for cz in (33.0, 21.8):
    ring = (cq.Workplane("YZ").circle(4.4).extrude(1.0)
            .translate((cx - 0.2, 105.75, cz)))
    ring = ring.cut(cq.Workplane("YZ").circle(3.4).extrude(1.0).translate((cx + 0.3, 105.75, cz)))
    body = body.union(ring)
for cy in (102.0, 109.5):
    for cz in (40.3, 14.6):
        body = body.union(cq.Workplane("YZ").polygon(6, 4.4).extrude(1.4)
                          .translate((cx - 0.2, cy, cz)))

# ---------------------------------------------------------------
# Bottom features
# ---------------------------------------------------------------
bb = (cq.Workplane("XY").circle(10.5).extrude(4.3).translate((BB_X, BB_Y, -5.5)))
bb = bb.union(cq.Workplane("XY").circle(9.3).extrude(5.0).translate((BB_X, BB_Y, -10.3)))
bb = bb.edges("<Z").chamfer(0.6)
body = body.union(bb)
body = body.cut(cq.Workplane("XY").circle(TP_HOLES[0][2] / 2).extrude(REC_Z0 + 20).translate((BB_X, BB_Y, -BP_T - 10)))

# lever mounting block
lm = (cq.Workplane("XY").polyline([(38.0, 29.0), (57.0, 29.0), (57.0, 66.0), (51.0, 72.0),
                                    (34.0, 72.0), (34.0, 46.0), (28.0, 46.0), (28.0, 39.0)])
      .close().extrude(1.6).translate((0, 0, -BP_T - 1.5)))
body = body.union(lm)
for hx in (38.5, 52.0):
    for hy in (39.5, 67.0):
        body = body.union(cq.Workplane("XY").circle(2.4).extrude(1.4).translate((hx, hy, -BP_T - 2.8)))
        body = body.cut(cq.Workplane("XY").circle(1.3).extrude(1.0).translate((hx, hy, -BP_T - 2.9)))


# lever: flat post with rounded lower end + cylindrical grip along +Y
lw = LEV_X1 - LEV_X0
lcx = (LEV_X0 + LEV_X1) / 2
lcz = LEV_BOT + lw / 2
ztop = -BP_T - 1.4
post = (cq.Workplane("XZ").moveTo(LEV_X0, ztop).lineTo(LEV_X0, lcz)
        .threePointArc((lcx, lcz - lw / 2), (LEV_X1, lcz)).lineTo(LEV_X1, ztop).close()
        .extrude(-(LEV_Y1 - LEV_Y0)).translate((0, LEV_Y0, 0)))
body = body.union(post)
grip_prof = [
    (0, LEV_Y1 - 1), (NECK_D / 2, LEV_Y1 - 1), (NECK_D / 2, 77.4), (GRIP_D / 2, 85.6),
    (GRIP_D / 2, GRIP_END_Y - 0.8), (GRIP_D / 2 - 0.8, GRIP_END_Y), (0, GRIP_END_Y),
]
grip = (cq.Workplane("XY").polyline(grip_prof).close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
        .translate((lcx, 0, lcz - GRIP_DROP)))
body = body.union(grip)

# ---------------------------------------------------------------
# Rail (bar) with dovetail notches
# ---------------------------------------------------------------
lapx = LNOTCH_X + (LNOTCH_DEPTH - BAR_LIP) * t
bar_pts = [
    (BAR_X0, BAR_LIP), (LNOTCH_X, BAR_LIP), (lapx, LNOTCH_DEPTH),
    (lapx + (LNOTCH_DEPTH - BAR_FRONT) * t, BAR_FRONT),
    (ax - (ay - BAR_FRONT) * t, BAR_FRONT), (ax, ay),
    (ax + (ay - BAR_LIP) * t, BAR_LIP), (BAR_X1, BAR_LIP),
    (BAR_X1, BAR_BACK), (BAR_X0, BAR_BACK),
]
bar = (cq.Workplane("XY").polyline(bar_pts).close().extrude(BAR_Z1 - BAR_Z0)
       .translate((0, 0, BAR_Z0)))
bar = bar.union(box(BAR_X0, BAR_X1, BAR_BACK - 0.1, RIB_BACK, RIB_Z0, RIB_Z1))

# rod
rod = (cq.Workplane("XZ").circle(ROD_D / 2).extrude(-(ROD_END_Y - BAR_BACK + 3))
       .translate((ROD_X, BAR_BACK - 3, ROD_Z)))
bar = bar.union(rod)

# knob on +X end
knob = (cq.Workplane("YZ").circle(KNOB_FL_D / 2).extrude(2.5)
        .translate((BAR_X1, KNOB_Y, KNOB_Z)))
knob = knob.intersect(box(BAR_X1 - 1, BAR_X1 + 5, KNOB_Y - 20, RIB_BACK, KNOB_Z - 20, KNOB_Z + 20))
knob = knob.union(cq.Workplane("YZ").circle(KNOB_D / 2 - 0.4).extrude(KNOB_L)
                  .translate((BAR_X1, KNOB_Y, KNOB_Z)))
knob = knob.cut(cq.Workplane("YZ").circle(KNOB_D).circle(KNOB_D / 2 - 1.2).extrude(1.4)
                .translate((BAR_X1 + 7.0, KNOB_Y, KNOB_Z)))
knob = knob.union(cq.Workplane("YZ").circle(KNOB_D / 2).extrude(KNOB_L - 8.4)
                  .translate((BAR_X1 + 8.4, KNOB_Y, KNOB_Z)))
knob = knob.cut(cq.Workplane("YZ").circle(3.0).extrude(1.0).translate((BAR_X1 + KNOB_L - 1.0, KNOB_Y, KNOB_Z)))
bar = bar.union(knob)

result = body.union(bar)
